import math
import cadquery as cq

# Flanged blind rivet nut with a conical shank.
# Axis = X.  Flange (head) at x = 0 facing -X, tapered shank runs to +X.

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 23.6        # flange outer diameter
FLANGE_RIM_T = 0.72    # flange thickness at the outer rim
FLANGE_RIM_R = 0.2     # rounding of the flange rim
FLANGE_CONE_R = 11.5   # radius where the conical underside of the flange starts
BODY_BASE_D = 16.1     # shank diameter where it meets the flange
BODY_BASE_X = 1.45     # axial position of the shank/flange junction
BODY_END_D = 12.9      # shank diameter at the tail end
LENGTH = 19.9          # overall length (flange face to tail end)
JUNCTION_FILLET = 0.6  # fillet between flange and conical shank

CB_D = 12.8            # counterbore diameter (head side)
CB_DEPTH = 5.2         # counterbore depth
CB_ENTRY_CH = 0.3      # chamfer at the counterbore mouth
CB_BOTTOM_CH = 0.95    # 45 deg chamfer at the counterbore bottom
BORE2_D = 10.9         # plain bore after the counterbore
BORE2_DEPTH = 10.0     # depth (from flange face) where the plain bore ends

SLOT_N = 6             # number of axial key slots in the counterbore
SLOT_W = 1.4           # slot width
SLOT_R = 7.0           # slot floor radius
SLOT_LEN = 6.15        # slot length (axial)
SLOT_RUNOUT_R = 0.6    # rounded run-out at the deep end of each slot
SLOT_ANGLE0 = 30.0     # angular position of first slot (deg, from +Y toward +Z)

THREAD_MINOR_D = 8.4   # thread minor (bore) diameter
THREAD_MAJOR_D = 10.0  # thread major diameter (M10 x 1.5)
THREAD_PITCH = 1.5
END_CSK_D = 9.35       # countersink diameter at the thread entrance
END_CSK_ANGLE = 120.0  # countersink included angle

OUTER_SEAM = -45.0     # where the revolve seams sit (cosmetic only)
TAIL_SEAM = 180.0


def revolve_x(pts, seam_deg=0.0):
    """Revolve a closed (x, r) profile drawn in the XY plane about the X axis.
    seam_deg turns the body about X so the revolve seam sits where it is least visible."""
    body = cq.Workplane("XY").polyline(pts).close().revolve(360.0, (0, 0, 0), (1, 0, 0))
    return body.rotate((0, 0, 0), (1, 0, 0), seam_deg) if seam_deg else body


rf = FLANGE_D / 2.0
rb = BODY_BASE_D / 2.0
re = BODY_END_D / 2.0
rcb = CB_D / 2.0
rb2 = BORE2_D / 2.0
rmin = THREAD_MINOR_D / 2.0
rmaj = THREAD_MAJOR_D / 2.0
rcs = END_CSK_D / 2.0

# ---------------- outer body by revolution ----------------
outer_pts = [
    (0.0, 0.0),
    (0.0, rf),
    (FLANGE_RIM_T, rf),
    (FLANGE_RIM_T + 0.05, FLANGE_CONE_R),
    (BODY_BASE_X, rb),
    (LENGTH, re),
    (LENGTH, 0.0),
]
solid = revolve_x(outer_pts, OUTER_SEAM)

# round the flange rim (the two circular edges at the outer diameter)
solid = solid.edges(
    cq.selectors.BoxSelector((-0.01, -rf - 0.01, -rf - 0.01), (FLANGE_RIM_T + 0.01, rf + 0.01, rf + 0.01))
).fillet(FLANGE_RIM_R)

# fillet where the conical shank meets the flange
solid = solid.edges(
    cq.selectors.BoxSelector((BODY_BASE_X - 0.01, -rb - 0.01, -rb - 0.01), (BODY_BASE_X + 0.01, rb + 0.01, rb + 0.01))
).fillet(JUNCTION_FILLET)

# ---------------- internal bore (head side + threaded side) ----------------
e = 0.05
head_pts = [
    (-e, 0.0),
    (-e, rcb + CB_ENTRY_CH + e),
    (CB_ENTRY_CH, rcb),                               # mouth chamfer
    (CB_DEPTH, rcb),                                  # counterbore wall
    (CB_DEPTH + CB_BOTTOM_CH, rcb - CB_BOTTOM_CH),    # bottom chamfer
]
if rb2 < rcb - CB_BOTTOM_CH - 1e-6:
    head_pts.append((CB_DEPTH + CB_BOTTOM_CH, rb2))
head_pts += [
    (BORE2_DEPTH, rb2),                               # plain bore
    (BORE2_DEPTH, 0.0),                               # flat step down to the thread
]
solid = solid.cut(revolve_x(head_pts))

tail_pts = [
    (BORE2_DEPTH - e, 0.0),
    (BORE2_DEPTH - e, rmin),
    (LENGTH - (rcs - rmin) / math.tan(math.radians(END_CSK_ANGLE / 2.0)), rmin),  # thread minor bore
    (LENGTH + e, rcs + e),                            # countersink at the tail
    (LENGTH + e, 0.0),
]
solid = solid.cut(revolve_x(tail_pts, TAIL_SEAM))

# ---------------- key slots in the counterbore wall ----------------
for i in range(SLOT_N):
    ang = SLOT_ANGLE0 + i * 360.0 / SLOT_N
    slot = (
        cq.Workplane("XY")
        .box(SLOT_LEN + 1.0, SLOT_R, SLOT_W, centered=(False, False, True))
        .translate((-1.0, 0, 0))
        .edges("|Z and >X and >Y")
        .fillet(SLOT_RUNOUT_R)
        .rotate((0, 0, 0), (1, 0, 0), ang)
    )
    solid = solid.cut(slot)

# ---------------- thread, represented by annular V grooves ----------------
n_grooves = int((LENGTH - BORE2_DEPTH) / THREAD_PITCH)   # thread runs up to the plain bore
for k in range(n_grooves):
    xc = LENGTH - THREAD_PITCH * (k + 0.5)
    # ISO-like 60 deg groove: 3P/4 wide at the minor diameter, P/8 flat at the root
    ring = revolve_x([
        (xc - THREAD_PITCH * 0.375, rmin - 0.01),
        (xc - THREAD_PITCH * 0.0625, rmaj),
        (xc + THREAD_PITCH * 0.0625, rmaj),
        (xc + THREAD_PITCH * 0.375, rmin - 0.01),
    ], TAIL_SEAM)
    solid = solid.cut(ring)

result = solid
